import math
import cadquery as cq

# =====================================================================
#  Four-engine wide-body airliner (747 style) model
#  Axes: X = span (right wing +X), Y = up (cabin roof +Y),
#        Z = fuselage axis, nose at Z = 0, tail towards +Z
# =====================================================================

# ---------------- fuselage (main body) ----------------
# The fuselage is one smooth loft through "egg" stations: an elliptic
# upper half (which also forms the upper-deck hump) and a super-elliptic
# lower half (boxy around the wing-body fairing).
# Station = (z, y of max width, half width, upper half-height,
#            lower half-height, lower super-ellipse exponent)
BF_EXP = 4.5          # super-elliptic belly (wing-body fairing) exponent
FUS_STATIONS = [
    (0.5, 2.0, 0.8, 1.0, 0.7, 2.0),
    (4.0, 2.0, 2.95, 5.0, 3.6, 2.0),
    (12.0, 1.5, 6.3, 10.2, 8.5, 2.0),
    (25.0, 1.0, 9.25, 15.1, 11.6, 2.0),
    (45.0, 0.6, 10.8, 16.25, 13.1, 2.0),
    (60.0, 0.55, 10.9, 16.3, 13.55, 2.4),    # hump ends / belly fairing starts
    (80.0, 0.55, 10.9, 14.2, 13.5, BF_EXP),
    (125.0, 0.55, 10.9, 13.75, 13.45, BF_EXP),
    (160.0, 1.9, 10.7, 12.4, 12.2, 2.0),     # tail upsweep begins
    (190.0, 4.5, 9.5, 10.1, 10.0, 2.0),
    (212.0, 6.3, 6.4, 8.7, 7.6, 2.0),
    (230.0, 6.0, 2.3, 3.6, 3.0, 2.0),        # blunt tail cone end
]
FUS_SECTION_PTS = 36
FUS_SEAM_DEG = 90.0   # loft seam along the roof centre line (under the fin)

# ---------------- wing ----------------
W_ROOT_X = 2.0        # wing root station (inside the fuselage)
W_KINK_X = 49.5       # trailing-edge kink station
W_TIP_X = 100.2       # wing tip station
W_STATIONS = (W_ROOT_X, 40.0, 60.0, W_TIP_X)   # loft stations (smooth TE kink)
W_LE_Z0 = 70.7        # leading edge Z at fuselage side (x = 10.7)
W_LE_SWEEP = 0.866    # dZ/dX of the leading edge
W_TE_Z0 = 120.4       # trailing edge Z at fuselage side
W_TE_IN = 0.327       # dZ/dX inboard trailing edge
W_TE_OUT = 0.572      # dZ/dX outboard trailing edge
W_YLOW0 = -7.0        # lower surface height at x = 10.5
W_DIHEDRAL = 0.078    # dY/dX of lower surface
W_TMAX_ROOT = 8.4     # max thickness at x = 10.5
W_TMAX_TIP = 4.6      # max thickness at the tip
W_TTE_ROOT = 3.7      # trailing edge (blunt) thickness at root
W_TTE_TIP = 3.7       # trailing edge thickness at tip

# ---------------- engines ----------------
ENG_X = [44.3, 72.8]
ENG_Y = [-9.2, -7.0]            # nacelle axis heights
ENG_ZF = [86.2, 112.4]          # intake face Z
ENG_R = 4.2
ENG_CYL_L = 8.4
ENG_TOTAL_L = 17.6
ENG_REAR_R = 1.5
PYLON_T = 0.7
PYLON_TE_GAP = 5.5              # pylon ends this far ahead of wing TE

# ---------------- flap-track fairings ----------------
FTF_X = [22.4, 33.7, 52.6, 65.2]
FTF_ZF = [101.4, 108.8, 119.3, 126.7]
FTF_AFT = 4.5        # overhang behind trailing edge
FTF_AFT_SLANT = 0.6  # forward lean of the fairing's aft edge (dZ/dY)
FTF_W = 2.4
FTF_DEPTH = 2.0

# ---------------- horizontal tail ----------------
HT_TIP_X = 36.9
HT_LE_Z0 = 194.8      # LE at x=0
HT_LE_SWEEP = 0.92
HT_TE_Z0 = 226.4
HT_TE_SWEEP = 0.283
HT_YLOW0 = 6.0
HT_DIHEDRAL = 0.197
HT_T_ROOT = 5.6
HT_T_TIP = 4.6

# ---------------- vertical fin ----------------
VF_ROOT_Y = 6.0
VF_TIP_Y = 48.3
VF_LE_Z_AT13 = 184.7
VF_LE_SLOPE = 1.125   # dZ/dY
VF_TE_Z_AT13 = 227.8
VF_TE_SLOPE = 0.249
VF_T_ROOT = 2.2
VF_T_TIP = 1.3


# ---------------------------------------------------------------------
# ---------------- fuselage body ----------------
def fus_section(z, yc, a, b_up, b_low, n_low):
    """Egg-shaped station: elliptic top, super-elliptic (boxy) bottom."""
    pts = []
    for i in range(FUS_SECTION_PTS):
        t = math.radians(FUS_SEAM_DEG + i * 360.0 / FUS_SECTION_PTS)
        c, s_ = math.cos(t), math.sin(t)
        if s_ >= 0:
            x, y = a * c, yc + b_up * s_
        else:
            e = 2.0 / n_low
            x = a * math.copysign(abs(c) ** e, c)
            y = yc - b_low * abs(s_) ** e
        pts.append(cq.Vector(x, y, z))
    params = [i / FUS_SECTION_PTS for i in range(FUS_SECTION_PTS + 1)]
    edge = cq.Edge.makeSpline(pts, periodic=True, parameters=params)
    return cq.Wire.assembleEdges([edge])


fus_body = cq.Solid.makeLoft([fus_section(*st) for st in FUS_STATIONS], False)


fuselage = cq.Workplane("XY").add(fus_body)


# ---------------- airfoil section helper ----------------
def airfoil(plane, y_low, z_le, chord, t_max, t_te, sym=False):
    """Closed airfoil wire in a plane whose local x is the thickness
    direction and local y is the chord direction (+Z)."""
    z_te = z_le + chord
    wp = cq.Workplane(plane)
    if not sym:
        r = 0.36 * t_max
        w = (wp.moveTo(y_low, z_te)
             .lineTo(y_low + t_te, z_te)
             .spline([(y_low + t_te + 0.65 * (t_max - t_te), z_le + 0.65 * chord),
                      (y_low + t_max, z_le + 0.33 * chord),
                      (y_low + 0.82 * t_max, z_le + 0.10 * chord),
                      (y_low + r, z_le)],
                     tangents=[(0.15, -1.0), (-1.0, 0.0)], includeCurrent=True)
             .threePointArc((y_low + r - 0.7071 * r, z_le + r - 0.7071 * r),
                            (y_low, z_le + r))
             .close())
    else:
        h = 0.5 * t_max
        ht = 0.5 * t_te
        w = (wp.moveTo(-ht, z_te)
             .lineTo(ht, z_te)
             .spline([(ht + 0.7 * (h - ht), z_le + 0.65 * chord),
                      (h, z_le + 0.33 * chord),
                      (0.75 * h, z_le + 0.08 * chord),
                      (0.0, z_le)],
                     tangents=[(0.15, -1.0), (-1.0, 0.0)], includeCurrent=True)
             .spline([(-0.75 * h, z_le + 0.08 * chord),
                      (-h, z_le + 0.33 * chord),
                      (-ht - 0.7 * (h - ht), z_le + 0.65 * chord),
                      (-ht, z_te)],
                     tangents=[(-1.0, 0.0), (0.15, 1.0)], includeCurrent=True)
             .close())
    return w.wires().val()


# ---------------- wing ----------------
def wing_le(x):
    return W_LE_Z0 + (x - 10.7) * W_LE_SWEEP


def wing_te(x):
    if x <= W_KINK_X:
        return W_TE_Z0 + (x - 10.7) * W_TE_IN
    return W_TE_Z0 + (W_KINK_X - 10.7) * W_TE_IN + (x - W_KINK_X) * W_TE_OUT


def wing_ylow(x):
    return W_YLOW0 + (x - 10.5) * W_DIHEDRAL


def lerp_span(x, a, b):
    f = (x - 10.5) / (W_TIP_X - 10.5)
    return a + (b - a) * f


def wing_tte(x):
    return lerp_span(x, W_TTE_ROOT, W_TTE_TIP)


def wing_wire(x, side=1):
    pl = cq.Plane(origin=(side * x, 0, 0), xDir=(0, 1, 0), normal=(1, 0, 0))
    return airfoil(pl, wing_ylow(x), wing_le(x), wing_te(x) - wing_le(x),
                   lerp_span(x, W_TMAX_ROOT, W_TMAX_TIP), wing_tte(x))


def make_wing(side):
    ws = [wing_wire(x, side) for x in W_STATIONS]
    return cq.Solid.makeLoft(ws, False)


wings = cq.Workplane("XY").add(make_wing(1)).union(make_wing(-1))


# ---------------- engines + pylons ----------------
def nacelle(x, ye, zf):
    r = ENG_R
    prof = [
        (0.0, zf + 1.2),
        (r * 0.80, zf + 1.2),
        (r * 0.80, zf),
        (r * 0.97, zf),
        (r, zf + 0.8),
        (r, zf + ENG_CYL_L - 0.6),
        (r * 0.95, zf + ENG_CYL_L),
        (r * 0.80, zf + ENG_CYL_L),
        (ENG_REAR_R, zf + ENG_TOTAL_L),
        (ENG_REAR_R * 0.65, zf + ENG_TOTAL_L),
        (0.0, zf + ENG_TOTAL_L + 1.4),
    ]
    pl = cq.Plane(origin=(x, ye, 0), xDir=(0, 1, 0), normal=(1, 0, 0))
    body = (cq.Workplane(pl).polyline(prof).close()
            .revolve(360, (0, 0, 0), (0, 1, 0)))
    # pylon: thin blade from nacelle up into the wing, running aft
    yl = wing_ylow(x)
    z_end = wing_te(x) - PYLON_TE_GAP
    pts = [
        (ye + 0.5 * r, zf + 3.0),
        (ye + 0.5 * r, zf + ENG_TOTAL_L - 3.0),
        (yl - 0.1, z_end),
        (yl + 1.5, z_end),
        (yl + 1.5, wing_le(x) + 2.0),
        (ye + r + 0.6, zf + 3.0),
    ]
    pl2 = cq.Plane(origin=(x - PYLON_T / 2, 0, 0), xDir=(0, 1, 0),
                   normal=(1, 0, 0))
    pylon = cq.Workplane(pl2).polyline(pts).close().extrude(PYLON_T)
    return body.union(pylon)


engines = None
for x, ye, zf in zip(ENG_X, ENG_Y, ENG_ZF):
    e = nacelle(x, ye, zf)
    e = e.union(e.mirror("YZ"))
    engines = e if engines is None else engines.union(e)


# ---------------- flap track fairings ----------------
def fairing(x, zf):
    """Canoe-shaped flap-track fairing: a smooth loft of elliptic stations
    hanging under the wing and running past the trailing edge."""
    yl = wing_ylow(x)
    zte = wing_te(x)
    tte = wing_tte(x)
    d = FTF_DEPTH
    hw = 0.5 * FTF_W

    def st(z, y0, y1, half_w):
        return cq.Wire.makeEllipse(half_w, 0.5 * (y1 - y0),
                                   cq.Vector(x, 0.5 * (y0 + y1), z),
                                   cq.Vector(0, 0, 1), cq.Vector(1, 0, 0))

    secs = [
        st(zf, yl - 0.1, yl + 0.9, 0.35 * hw),
        st(zf + 0.4 * (zte - zf), yl - 0.75 * d, yl + 1.5, 0.9 * hw),
        st(zte - 1.0, yl - d, yl + tte + 1.3, hw),
        st(zte + FTF_AFT, yl - 0.3 * d, yl + tte + 0.6, 0.6 * hw),
    ]
    return cq.Workplane("XY").add(cq.Solid.makeLoft(secs, False))


fairings = None
for x, zf in zip(FTF_X, FTF_ZF):
    f = fairing(x, zf)
    f = f.union(f.mirror("YZ"))
    fairings = f if fairings is None else fairings.union(f)


# ---------------- horizontal stabiliser ----------------
def ht_wire(x, side):
    pl = cq.Plane(origin=(side * x, 0, 0), xDir=(0, 1, 0), normal=(1, 0, 0))
    zle = HT_LE_Z0 + x * HT_LE_SWEEP
    zte = HT_TE_Z0 + x * HT_TE_SWEEP
    f = x / HT_TIP_X
    t = HT_T_ROOT + (HT_T_TIP - HT_T_ROOT) * f
    return airfoil(pl, HT_YLOW0 + x * HT_DIHEDRAL, zle, zte - zle, t, 0.7 * t)


htail = None
for s in (1, -1):
    h = cq.Solid.makeLoft([ht_wire(0.0, s), ht_wire(HT_TIP_X, s)], True)
    htail = cq.Workplane("XY").add(h) if htail is None else htail.union(h)


# ---------------- vertical fin ----------------
def vf_wire(y):
    pl = cq.Plane(origin=(0, y, 0), xDir=(-1, 0, 0), normal=(0, 1, 0))
    zle = VF_LE_Z_AT13 + (y - 13.0) * VF_LE_SLOPE
    zte = VF_TE_Z_AT13 + (y - 13.0) * VF_TE_SLOPE
    f = (y - VF_ROOT_Y) / (VF_TIP_Y - VF_ROOT_Y)
    t = VF_T_ROOT + (VF_T_TIP - VF_T_ROOT) * f
    return airfoil(pl, 0.0, zle, zte - zle, t, 0.6 * t, sym=True)


fin = cq.Solid.makeLoft([vf_wire(VF_ROOT_Y), vf_wire(VF_TIP_Y)], True)

# ---------------- assemble ----------------
result = (fuselage.union(wings).union(engines).union(fairings)
          .union(htail).union(cq.Workplane("XY").add(fin)))

VIEW = {"azimuth": 45, "elevation": 26}
